import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W_FOOT = 200.0      # overall width in X (outer faces of the vertical feet)
W_TOP = 155.0       # width of the top plate (outer mould line, virtual sharps)
LEG_INSET = 0.7     # leg bottoms sit this far inside the outer faces of the feet
DEPTH = 120.5       # length of the bracket along Y
HEIGHT = 60.3       # overall height (bottom of flanges to top of plate)
T_TOP = 2.8         # thickness of the top plate
T_LEG = 3.6         # thickness of the slanted legs
R_IN = 2.0          # inner bend radius (top bends)
R_OUT = 1.2         # outer bend radius (top bends)
EDGE_R = 1.0        # rounding of the outer sheet edges at the two open ends

FOOT_H = 6.3        # height of the vertical foot below the legs
T_FOOT = 1.1        # thickness of the foot / bottom return flange
FLANGE = 4.6        # length of the inward bottom flange (from outer face)
FOOT_R = 0.8        # outer radius of the foot/flange corner

# slots in the top plate (asymmetric in X)
SLOT_X = (-51.6, 62.8)
SLOT_Y = -2.8
SLOT_LEN = 90.8
SLOT_W = 12.3

# holes in the legs: (height of centre above ground, Y, through diameter)
HOLE_FILLET = 2.0   # rounded lip on the outside of every leg hole
HOLE_FILLET_IN = 1.1  # smaller rounding on the inside of every leg hole
LEFT_HOLES = [(18.9, 41.8, 17.5), (18.9, -41.8, 17.5),
              (46.4, 41.8, 17.5), (46.4, -41.8, 17.5)]
RIGHT_HOLES = [(36.0, 0.0, 25.0), (19.0, 36.4, 17.5), (19.0, -36.4, 17.5)]

# lettering cut right through the -X leg
TEXT = "DUKE"
TEXT_SIZE = 15.5
TEXT_Y = 0.0
TEXT_Z = 32.6       # height of the text centre
FONT = "DejaVu Serif"

VIEW = {"azimuth": 45, "elevation": 26}

xf = W_FOOT / 2.0                 # outer face of the feet
xo, xt = xf - LEG_INSET, W_TOP / 2.0  # leg bottom / leg top (outer surface)
LEG_DX, LEG_DZ = xo - xt, HEIGHT - FOOT_H
LEG_L = math.hypot(LEG_DX, LEG_DZ)
SIN_A, COS_A = LEG_DX / LEG_L, LEG_DZ / LEG_L      # leg angle from vertical


# ---------------- helpers ----------------
def offset_polyline(pts, ds):
    """Offset an open polyline to its right-hand side by ds[i] per segment (mitred joins)."""
    lines = []
    for ((x0, z0), (x1, z1)), d in zip(zip(pts[:-1], pts[1:]), ds):
        dx, dz = x1 - x0, z1 - z0
        L = math.hypot(dx, dz)
        nx, nz = dz / L, -dx / L
        lines.append(((x0 + nx * d, z0 + nz * d), (x1 + nx * d, z1 + nz * d)))
    out = [lines[0][0]]
    for (a0, a1), (b0, b1) in zip(lines[:-1], lines[1:]):
        x1, y1 = a0
        x2, y2 = a1
        x3, y3 = b0
        x4, y4 = b1
        den = (x1 - x2) * (y3 - y4) - (y1 - y2) * (x3 - x4)
        px = ((x1 * y2 - y1 * x2) * (x3 - x4) - (x1 - x2) * (x3 * y4 - y3 * x4)) / den
        py = ((x1 * y2 - y1 * x2) * (y3 - y4) - (y1 - y2) * (x3 * y4 - y3 * x4)) / den
        out.append((px, py))
    out.append(lines[-1][1])
    return out


def at_height(p0, p1, z):
    """Point on the line p0-p1 at height z."""
    t = (z - p0[1]) / (p1[1] - p0[1])
    return (p0[0] + t * (p1[0] - p0[0]), z)


def dist_to_polyline(x, z, pts):
    best = 1e9
    for (x0, z0), (x1, z1) in zip(pts[:-1], pts[1:]):
        dx, dz = x1 - x0, z1 - z0
        L2 = dx * dx + dz * dz
        t = max(0.0, min(1.0, ((x - x0) * dx + (z - z0) * dz) / L2))
        best = min(best, math.hypot(x - (x0 + t * dx), z - (z0 + t * dz)))
    return best


def select(wp, edges):
    return wp.newObject(edges)


# ---------------- main sheet: top plate + two slanted legs ----------------
outer = [(-xo, FOOT_H), (-xt, HEIGHT), (xt, HEIGHT), (xo, FOOT_H)]
inner_raw = offset_polyline(outer, (T_LEG, T_TOP, T_LEG))
# cut the legs off horizontally at the foot height
inner = ([at_height(inner_raw[0], inner_raw[1], FOOT_H)] + inner_raw[1:-1]
         + [at_height(inner_raw[-2], inner_raw[-1], FOOT_H)])
profile = outer + list(reversed(inner))

sheet = (
    cq.Workplane("XZ", origin=(0, DEPTH / 2.0, 0))
    .polyline(profile)
    .close()
    .extrude(DEPTH)
)

# bends
for (x, z) in inner[1:-1]:
    sheet = sheet.edges("|Y").edges(cq.selectors.NearestToPointSelector((x, 0.0, z))).fillet(R_IN)
for (x, z) in outer[1:-1]:
    sheet = sheet.edges("|Y").edges(cq.selectors.NearestToPointSelector((x, 0.0, z))).fillet(R_OUT)

# round the outer-surface edges of the two open ends
end_edges = []
for e in sheet.val().Edges():
    c = e.Center()
    if abs(abs(c.y) - DEPTH / 2.0) > 1e-3:
        continue
    v = [p.toTuple() for p in (e.startPoint(), e.endPoint())]
    if all(abs(p[2] - FOOT_H) < 1e-4 for p in v):
        continue  # bottom cut of the leg
    if dist_to_polyline(c.x, c.z, inner) > T_TOP * 0.6:
        end_edges.append(e)
sheet = select(sheet, end_edges).fillet(EDGE_R)


# ---------------- holes in the legs ----------------
def leg_point(side, z):
    """Point on the outer surface of a leg at height z, and the outward normal."""
    sgn = -1.0 if side == "left" else 1.0
    x = sgn * (xo - (z - FOOT_H) * LEG_DX / LEG_DZ)
    n = (sgn * COS_A, SIN_A)
    return x, n


hole_specs = []
for side, holes in (("left", LEFT_HOLES), ("right", RIGHT_HOLES)):
    for z, y, dia in holes:
        x, n = leg_point(side, z)
        start = cq.Vector(x + n[0] * 2.0, y, z + n[1] * 2.0)
        direction = cq.Vector(-n[0], 0, -n[1])
        cyl = cq.Solid.makeCylinder(dia / 2.0, T_LEG + 6.0, start, direction)
        sheet = sheet.cut(cq.Workplane().add(cyl))
        hole_specs.append((cq.Vector(x, y, z), cq.Vector(n[0], 0, n[1]), dia))

# rounded lips on both sides of each hole
def hole_edges(shape, depth):
    found = []
    for e in shape.val().Edges():
        if e.geomType() == "LINE":
            continue
        c = e.Center()
        for p, n, dia in hole_specs:
            if (c - (p - n * depth)).Length < 0.3:
                found.append(e)
    return found


sheet = select(sheet, hole_edges(sheet, T_LEG)).fillet(HOLE_FILLET_IN)
sheet = select(sheet, hole_edges(sheet, 0.0)).fillet(HOLE_FILLET)

# ---------------- slots in the top plate ----------------
for sx in SLOT_X:
    cutter = (
        cq.Workplane("XY", origin=(sx, SLOT_Y, HEIGHT - T_TOP - 1.0))
        .slot2D(SLOT_LEN, SLOT_W, angle=90)
        .extrude(T_TOP + 2.0)
    )
    sheet = sheet.cut(cutter)

# ---------------- feet: thin vertical strip with inward return flange ----------------
OV = 0.8  # overlap into the leg
tan_a = LEG_DX / LEG_DZ
foot_l = [
    (-xf, 0.0),
    (-xf, FOOT_H),
    (-xo, FOOT_H),
    (-xo + tan_a * OV, FOOT_H + OV),
    (-xf + T_FOOT + LEG_INSET, FOOT_H + OV),
    (-xf + T_FOOT + LEG_INSET, FOOT_H),
    (-xf + T_FOOT, FOOT_H),
    (-xf + T_FOOT, T_FOOT),
    (-xf + FLANGE, T_FOOT),
    (-xf + FLANGE, 0.0),
]
foot_r = [(-x, z) for (x, z) in reversed(foot_l)]
for pts in (foot_l, foot_r):
    f = (
        cq.Workplane("XZ", origin=(0, DEPTH / 2.0, 0))
        .polyline(pts)
        .close()
        .extrude(DEPTH)
    )
    sx = -1.0 if pts is foot_l else 1.0
    f = f.edges("|Y").edges(cq.selectors.NearestToPointSelector((sx * xf, 0.0, 0.0))).fillet(FOOT_R)
    sheet = sheet.union(f)

# ---------------- lettering cut through the -X leg ----------------
x_txt, n_txt = leg_point("left", TEXT_Z)
nvec = cq.Vector(n_txt[0], 0, n_txt[1])
txt_origin = cq.Vector(x_txt, TEXT_Y, TEXT_Z) - nvec * (T_LEG + 0.6)
plane_txt = cq.Plane(origin=txt_origin.toTuple(), xDir=(0, -1, 0), normal=nvec.toTuple())
letters = cq.Workplane(plane_txt).text(TEXT, TEXT_SIZE, T_LEG + 1.2, font=FONT, kind="bold",
                                        halign="center", valign="center")
sheet = sheet.cut(letters)

result = sheet
